import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 120.0        # outer length of the tub (X)
D = 62.5         # outer depth of the tub (Y)
H = 68.5         # overall height (Z), floor bottom to wall top
T = 3.3          # wall thickness (front/back/end walls)
TF = 3.0         # floor thickness
N = 3            # number of compartments
DIV = 4.8        # divider thickness (X)
DIV_H = 8.0      # height of the low divider rib (from floor bottom)
BLK = 4.3        # how far the full-height divider posts stand proud of the wall

SLOT_W = 9.7     # width of the U-slots in front/back walls
SLOT_D = 24.5    # depth of the U-slots from the wall top (incl. round bottom)

HOLE_D = 20.5    # floor hole diameter (one per compartment, centred)

FL = 9.5         # end flange overhang (45 deg triangular flange, full depth)
FH_D = 4.6       # flange mounting hole diameter
FH_Y = 11.0      # flange hole distance from front/back faces

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
inner_w = W - 2 * T
inner_d = D - 2 * T
COMP = (inner_w - (N - 1) * DIV) / N      # clear width of one compartment
x0 = -W / 2 + T                           # inner face of the -X end wall


def comp_left(i):
    """X of the low-X boundary of compartment i."""
    return x0 + i * (COMP + DIV)


# ---------------- open-top tub ----------------
body = cq.Workplane("XY").box(W, D, H, centered=(True, True, False))
cavity = (
    cq.Workplane("XY")
    .workplane(offset=TF)
    .box(inner_w, inner_d, H, centered=(True, True, False))
)
body = body.cut(cavity)

# ---------------- dividers: low floor rib + full-height posts at the walls ----------------
for i in range(1, N):
    xc = comp_left(i) - DIV / 2
    rib = (
        cq.Workplane("XY")
        .box(DIV, inner_d + 0.02, DIV_H, centered=(True, True, False))
        .translate((xc, 0, 0))
    )
    body = body.union(rib)
    for sgn in (-1, 1):
        yc = sgn * (D / 2 - T - BLK / 2 + 0.01)
        post = (
            cq.Workplane("XY")
            .box(DIV, BLK + 0.02, H, centered=(True, True, False))
            .translate((xc, yc, 0))
        )
        body = body.union(post)

# ---------------- U-slots through front and back walls ----------------
r = SLOT_W / 2
for i in range(N):
    xs = comp_left(i) + r                 # slot hugs the low-X side of each compartment
    zc = H - SLOT_D + r                   # centre of the round bottom
    prof = (
        cq.Workplane("XZ")
        .moveTo(xs - r, H + 1.0)
        .lineTo(xs - r, zc)
        .threePointArc((xs, zc - r), (xs + r, zc))
        .lineTo(xs + r, H + 1.0)
        .close()
    )
    slot = prof.extrude(D, both=True)
    body = body.cut(slot)

# ---------------- floor holes ----------------
for i in range(N):
    xc = comp_left(i) + COMP / 2
    hole = (
        cq.Workplane("XY")
        .center(xc, 0)
        .circle(HOLE_D / 2)
        .extrude(TF + 2)
        .translate((0, 0, -1))
    )
    body = body.cut(hole)

# ---------------- end flanges: 45 deg triangular ledges with two holes each ----------------
for sgn in (-1, 1):
    xw = sgn * W / 2
    tri = [(xw, H), (xw + sgn * FL, H), (xw, H - FL)]
    flange = cq.Workplane("XZ").polyline(tri).close().extrude(D / 2, both=True)
    xh = xw + sgn * FL / 2
    for yy in (-D / 2 + FH_Y, D / 2 - FH_Y):
        hole = (
            cq.Workplane("XY")
            .center(xh, yy)
            .circle(FH_D / 2)
            .extrude(FL + 2)
            .translate((0, 0, H - FL - 1))
        )
        flange = flange.cut(hole)
    body = body.union(flange)

result = body.clean()
